import math
import cadquery as cq

# =====================================================================
#  Curved hollow cover (arm-rest like shell) with a half-round stub.
#  Open at the bottom (Z = 0), +Y is the long direction, the body bends
#  toward +X and ends in a half-cylinder stub pointing along +X.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
T = 3.0            # wall thickness

# rounded nose: spheroid (axis along Y) cut at the seam with the lofted body
NOSE_CX = 26.8     # nose centre X
NOSE_A = 17.0      # spheroid semi axis along Y (front of the nose at Y = 0)
NOSE_R = 27.7      # spheroid radius (X and Z)
NOSE_SEAM = 13.0   # Y of the seam between nose and lofted body

# half-cylinder stub
STUB_R = 20.0      # stub radius
STUB_Y = 179.8     # stub axis Y
STUB_X_END = 117.3 # stub end face X
# end plane of the lofted body (vertical plane through two base points)
END_OUT = (100.0, 199.6)
END_IN = (88.8, 160.0)

# intermediate loft sections of the body:
# (foot X, foot Y, spine angle deg from +Y toward +X, outer half width, inner half width, height)
SECTIONS_MID = [
    (33.0, 48.0, 5.0, 32.3, 28.0, 31.0),
    (42.0, 85.0, 10.0, 36.5, 22.8, 31.6),
    (55.0, 115.0, 22.0, 41.0, 13.8, 29.7),
    (69.0, 143.0, 37.0, 36.5, 10.7, 26.7),
    (84.0, 170.0, 75.0, 22.4, 12.8, 23.3),
]

# screw bosses
BOSS1 = (28.6, 42.5)
BOSS2 = (59.8, 151.1)
BOSS_D = 16.0
HOLE_D = 5.2
HOLE_STEP_D = 6.8  # short step below the counterbore floor
CBORE_D = 12.0     # counterbore on the outside
CBORE_DEPTH = 8.0
BOSS_Z0 = 0.8      # bottom of the screw bosses
BOSS_CB_D = 10.0   # counterbore at the bottom of the bosses
BOSS_CB_DEPTH = 1.0

# rim rabbet
LIP_W = 1.5        # rabbet width along the bottom rim (taken from the inside of the wall)
LIP_H = 2.0        # rabbet height

# stub end details
CH_LEN = 14.0      # U-shaped frame around the cable notch behind the stub end wall
CH_W = 16.6
CH_H = 9.0
CH_WALL = 1.4
NOTCH_R = 5.5      # half-round notch (pocket) in the stub end face
NOTCH_D = 6.0      # length of the half-cylinder shell backing the notch pocket
WIN_R = 15.5       # window in the stub end face: outer arc radius
WIN_CUT = 9.8      # ... and offset of its straight side from the stub axis (-Y side)
RIB_T = 1.5        # rib along the stub forming the wire channel behind the window
RIB_X0 = 90.0

# snap tab inside the nose (horizontal plate at rim level with a hook)
TAB_X = 24.5
TAB_W = 9.0
TAB_LEN = 11.0
TAB_T = 1.6
HOOK_H = 3.0


# ---------------------------------------------------------------------
def nose_seam_radius(off=0.0):
    a = NOSE_A - off
    r = NOSE_R - off
    d = NOSE_A - NOSE_SEAM
    return r * math.sqrt(1.0 - (d / a) ** 2)


def section_wire(fx, fy, ang, a_o, a_i, h):
    """Vertical section: smooth dome from the outer base point over the crown to the inner base point.
    The dome is one spline through points of two quarter ellipses (outer / inner half widths) with
    matching derivatives; the crown always sits at parameter 0.5 so that all sections loft consistently."""
    r = math.radians(ang)
    u = cq.Vector(math.cos(r), -math.sin(r), 0)  # from outer side to inner side
    z = cq.Vector(0, 0, 1)
    c = cq.Vector(fx, fy, 0)
    pts = []
    tans = []
    degs = (180, 150, 120, 90, 60, 30, 0)
    for deg in degs:
        t = math.radians(deg)
        a = a_o if deg > 90 else a_i
        if deg == 90:
            a = 0.5 * (a_o + a_i)
        pts.append(c + u * (a * math.cos(t)) + z * (h * math.sin(t)))
        tans.append((u * (a * math.sin(t)) - z * (h * math.cos(t))) * math.pi)
    params = [k / (len(degs) - 1.0) for k in range(len(degs))]
    dome = cq.Edge.makeSpline(pts, tangents=tans, parameters=params, scale=False)
    base = cq.Edge.makeLine(pts[-1], pts[0])
    return cq.Wire.assembleEdges([dome, base])


def exact_wire(fx, fy, ang, a, h):
    """Half ellipse section (exact), oriented like section_wire (outer -> crown -> inner)."""
    r = math.radians(ang)
    u = cq.Vector(math.cos(r), -math.sin(r), 0)
    c = cq.Vector(fx, fy, 0)
    xd = u * -1.0
    dome = cq.Edge.makeEllipse(a, h, c, xd.cross(cq.Vector(0, 0, 1)), xd, 0, 180)
    base = cq.Edge.makeLine(c + u * a, c - u * a)
    return cq.Wire.assembleEdges([dome, base])


def end_section():
    ox, oy = END_OUT
    ix, iy = END_IN
    cx, cy = (ox + ix) / 2, (oy + iy) / 2
    dx, dy = ix - ox, iy - oy
    ang = math.degrees(math.atan2(dy, dx))  # direction of u
    # exact section of the stub cylinder (axis along X) by the vertical end plane
    half = STUB_R / abs(dy / math.hypot(dx, dy))
    return (cx, cy, -ang, half, STUB_R)


def body_solid(off=0.0):
    """Lofted body from the nose seam to the end plane; exact half ellipses at both ends so the
    nose and the stub fuse onto identical faces."""
    rs = nose_seam_radius(0.0)
    wires = [exact_wire(NOSE_CX, NOSE_SEAM, 0.0, rs - off, rs - off)]
    for (fx, fy, ang, a_o, a_i, h) in SECTIONS_MID:
        wires.append(section_wire(fx, fy, ang, a_o - off, a_i - off, h - off))
    cx, cy, ang, half, h = end_section()
    # the stub cylinder of radius R - off cut by the end plane gives half widths scaled the same way
    k = (STUB_R - off) / STUB_R
    wires.append(exact_wire(cx, cy, ang, half * k, h - off))
    loft = cq.Solid.makeLoft(wires, False)
    return cq.Workplane("XY").add(loft)


def nose_solid(off=0.0):
    """Spheroid nose (axis along Y), offset inwards by 'off', cut at the seam plane.
    The inner spheroid keeps its front at Y = off and meets the offset loft section exactly."""
    a = NOSE_A - off
    d = NOSE_A - NOSE_SEAM
    b = (nose_seam_radius(0.0) - off) / math.sqrt(1.0 - (d / a) ** 2)
    wp = cq.Workplane("YZ", origin=(NOSE_CX, 0, 0))
    sph = (wp.moveTo(NOSE_A + a, 0).ellipseArc(a, b, 0, 180).close()
           .revolve(360, (0, 0, 0), (1, 0, 0)))
    cut = (cq.Workplane("XY").box(200, NOSE_SEAM + 1.0, 100, centered=(True, False, False))
           .translate((NOSE_CX, -1.0, 0)))
    return sph.intersect(cut)


def end_plane_box():
    """Big box occupying the half space beyond the loft end plane."""
    ox, oy = END_OUT
    ix, iy = END_IN
    cx, cy = (ox + ix) / 2, (oy + iy) / 2
    ang = math.degrees(math.atan2(iy - oy, ix - ox))
    return (cq.Workplane("XY").box(200, 200, 200, centered=(False, True, True))
            .rotate((0, 0, 0), (0, 0, 1), ang + 90)
            .translate((cx, cy, 0)))


def upper_half():
    return cq.Workplane("XY").box(400, 400, 100, centered=(True, True, False))


def stub_solid(off=0.0):
    r = STUB_R - off
    x0 = 70.0
    cyl = (cq.Workplane("YZ", origin=(x0, STUB_Y, 0)).circle(r)
           .extrude(STUB_X_END - off - x0))
    return cyl.intersect(upper_half()).intersect(end_plane_box())


def skin(off=0.0):
    return body_solid(off).union(nose_solid(off)).union(stub_solid(off))


def cyl_z(x, y, d, z0, z1):
    return cq.Workplane("XY").workplane(offset=z0).center(x, y).circle(d / 2.0).extrude(z1 - z0)


def slab(z0, z1):
    return cq.Workplane("XY").box(400, 400, z1 - z0, centered=(True, True, False)).translate((0, 0, z0))


# ---------------- outer skin and hollow ----------------
outer = skin()
cavity = skin(T).translate((0, 0, -0.01))
part = outer.cut(cavity)

# rabbet (inner step) along the bottom rim
lip = skin(T - LIP_W).intersect(slab(-1.0, LIP_H))
part = part.cut(lip)

# ---------------- screw bosses with counterbored holes ----------------
for (bx, by) in (BOSS1, BOSS2):
    boss = cyl_z(bx, by, BOSS_D, BOSS_Z0, 60.0).intersect(outer)
    part = part.union(boss)
for (bx, by) in (BOSS1, BOSS2):
    ztop = cyl_z(bx, by, 0.5, 0.0, 60.0).intersect(outer).val().BoundingBox().zmax
    part = part.cut(cyl_z(bx, by, CBORE_D, ztop - CBORE_DEPTH, 60.0))
    part = part.cut(cyl_z(bx, by, HOLE_STEP_D, ztop - CBORE_DEPTH - 1.5, 60.0))
    part = part.cut(cyl_z(bx, by, HOLE_D, -1.0, 60.0))
    part = part.cut(cyl_z(bx, by, BOSS_CB_D, -1.0, BOSS_Z0 + BOSS_CB_DEPTH))

# ---------------- stub end details ----------------
xe = STUB_X_END
# rib along the stub: wire channel between the rib and the -Y wall, its face flush with the window side
rib = (cq.Workplane("XY").box(xe - RIB_X0, RIB_T, 40, centered=(False, False, False))
       .translate((RIB_X0, STUB_Y - WIN_CUT, 0)))
part = part.union(rib.intersect(stub_solid(T / 2)))
# U-shaped frame behind the end wall, around the half-round notch pocket
frame = (cq.Workplane("XY").box(CH_LEN, CH_W, CH_H, centered=(False, True, False))
         .translate((xe - T - CH_LEN + 0.5, STUB_Y, 0)))
frame_in = (cq.Workplane("XY").box(CH_LEN, CH_W - 2 * CH_WALL, CH_H + 2, centered=(False, True, False))
            .translate((xe - T - CH_LEN + 0.5 + CH_WALL, STUB_Y, -1)))
part = part.union(frame.cut(frame_in).intersect(stub_solid(T / 2)))
# half-round pocket in the end face, backed by a half-cylinder shell
shell = (cq.Workplane("YZ", origin=(xe - T - NOTCH_D + 0.5, STUB_Y, 0))
         .circle(NOTCH_R + CH_WALL).extrude(NOTCH_D).intersect(upper_half()))
part = part.union(shell)
notch = (cq.Workplane("YZ", origin=(xe - T - NOTCH_D + 0.5 + CH_WALL, STUB_Y, 0)).circle(NOTCH_R)
         .extrude(NOTCH_D + T + 2.0))
part = part.cut(notch)
# window in the end wall (between an inner arc and a vertical line, on the -Y side)
win = (cq.Workplane("YZ", origin=(xe - T - 1.0, STUB_Y, 0)).circle(WIN_R).extrude(T + 3.0)
       .intersect(cq.Workplane("XY").box(50, 50, 50, centered=(True, False, False))
                  .translate((xe, STUB_Y - WIN_CUT - 50, 0))))
part = part.cut(win)

# ---------------- snap tab inside the nose ----------------
tab = (cq.Workplane("XY").box(TAB_W, TAB_LEN + 3.0, TAB_T, centered=(True, False, False))
       .translate((TAB_X, T - 3.0 + 0.5, 0)))
hook = (cq.Workplane("XY").box(TAB_W, 1.6, HOOK_H, centered=(True, False, False))
        .translate((TAB_X, T + TAB_LEN - 1.6, 0)))
part = part.union(tab.union(hook).intersect(skin(0.3)))

result = part

VIEW = {"azimuth": 45, "elevation": 26}
